import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 100.0      # overall width  (X)
H = 77.5       # overall height (Z)
D = 34.3       # overall depth  (Y); front face at Y=0, open back at Y=D
T = 2.0        # side / top / bottom wall thickness
TF = 2.0       # front wall thickness

XI = W / 2 - T     # inner half width
ZI = H / 2 - T     # inner half height

# display window (through the front wall)
WIN_W = 79.8
WIN_H = 27.4
WIN_ZC = H / 2 - 27.1          # window centre height
NOTCH_X = 45.6                 # notch tip x (right side, +X)
NOTCH_IN = 8.6                 # half height of notch at window edge
NOTCH_OUT = 3.1                # half height of notch flat

# mounting holes around the window
HOLE_D = 3.4
HOLE_DX = 41.55
HOLE_DZ = 17.15

# shallow label pocket
POCK_W = 66.8
POCK_H = 11.2
POCK_ZC = H / 2 - 61.1
POCK_DEPTH = 0.6

# back cover seat: posts and catch stop this far inside the rim
COVER_T = 2.0
Y_SEAT = D - COVER_T

# corner screw posts for the back cover
POST_BOSS_R = 4.0      # boss radius around the screw hole (merges into the walls)
POST_HOLE_D = 1.8      # pilot hole
POST_HX = 3.8          # hole offset from side wall inner face
POST_HZ = 3.6          # hole offset from top/bottom wall inner face
POST_Y0_TOP = 9.0      # front end of the upper posts
POST_HX_LOW = 3.7      # lower hole offset from side wall inner face
POST_HZ_LOW = 3.75     # lower hole offset from floor
POST_HOLE_DEPTH = 8.0  # blind pilot hole depth

# side support blocks (left/right inner walls, lower half)
SB_W = 5.2             # protrusion from side wall
SB_Z0 = -25.8          # bottom of block
SB_Z1 = -15.0          # top of block
LOW_W_TOP = 11.2       # pedestal ledge protrusion from side wall (top)
LOW_W_BOT = 9.0        # pedestal protrusion at its lower edge
LOW_Z = -33.0          # lower edge of the pedestal
WEB_W = 5.0            # web from pedestal down to the floor
PED_Y0 = 20.0          # front end of the rear pedestal
COL_X = 6.8            # round column: distance of axis from side wall
COL_Y = 11.6           # round column: distance of axis from front face
COL_R = 4.5
LIP_W = 1.2            # lip along the pedestal's lower edge
LIP_H = 0.8

# centre post on the inner front wall
CP_W = 4.2
CP_D = 3.6

# snap catch under the ceiling near the back opening
CATCH_X0 = -17.5
CATCH_XS = 5.5         # step in the catch
CATCH_X1 = 15.5
CATCH_Y0 = 19.5
CATCH_Y0B = 22.0       # front of the narrower (+X) segment
CATCH_H = 3.6

VIEW = {"azimuth": 45, "elevation": 26}


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0)
            .translate(((x0 + x1) / 2, (y0 + y1) / 2, (z0 + z1) / 2)))


def yz_prism(pts, x0, x1):
    """Prism from a polygon in the YZ plane, spanning x0..x1."""
    return (cq.Workplane("YZ", origin=(x0, 0, 0))
            .polyline(pts).close()
            .extrude(x1 - x0))


# ---------------- main shell (open back) ----------------
body = box(-W / 2, W / 2, 0, D, -H / 2, H / 2)
body = body.cut(box(-XI, XI, TF, D + 1, -ZI, ZI))

# ---------------- upper corner screw posts ----------------
post_holes = []
for sx in (-1, 1):
    sz = 1
    y0 = POST_Y0_TOP
    cx, cz = sx * XI, sz * ZI
    hx, hz = cx - sx * POST_HX, cz - sz * POST_HZ
    p = (cq.Workplane("XZ", origin=(0, Y_SEAT, 0))
         .center(hx, hz).circle(POST_BOSS_R)
         .extrude(Y_SEAT - y0))
    p = p.union(box(min(hx, cx + sx * 0.01), max(hx, cx + sx * 0.01), y0, Y_SEAT,
                    hz, cz + 0.01))
    # 45 deg lead-in on the front end of the hanging posts
    s_ = POST_HZ + POST_BOSS_R + 0.5
    cut = yz_prism([(y0 - 1.0, cz + 1.0), (y0 + 1.0, cz + 1.0),
                    (y0 + s_ + 1.0, cz - s_), (y0 - 1.0, cz - s_)], -W, W)
    body = body.union(p.cut(cut))
    post_holes.append((hx, hz))

# ---------------- side support blocks (also carry the lower screw holes) ----------------
for sx in (-1, 1):
    xo = sx * XI
    # upper block (shelf support)
    blk = box(min(xo, xo - sx * SB_W), max(xo, xo - sx * SB_W),
              TF - 0.01, Y_SEAT, SB_Z0, SB_Z1)
    body = body.union(blk)
    # narrow web from the floor up to a thin shelf at LOW_Z (full length)
    web = box(min(xo + sx * 0.01, xo - sx * WEB_W), max(xo + sx * 0.01, xo - sx * WEB_W),
              TF - 0.01, Y_SEAT, -ZI - 0.01, LOW_Z + 0.01)
    shelf_w = LOW_W_BOT + LIP_W
    shelf = box(min(xo + sx * 0.01, xo - sx * shelf_w), max(xo + sx * 0.01, xo - sx * shelf_w),
                TF - 0.01, Y_SEAT, LOW_Z, LOW_Z + LIP_H)
    body = body.union(web).union(shelf)
    # rear pedestal: wide ledge under the block, inner face leaning toward the wall
    prof = [(xo + sx * 0.01, SB_Z0 + 0.01),
            (xo - sx * LOW_W_TOP, SB_Z0 + 0.01),
            (xo - sx * LOW_W_BOT, LOW_Z + 0.01),
            (xo + sx * 0.01, LOW_Z + 0.01)]
    ped = (cq.Workplane("XZ", origin=(0, PED_Y0, 0))
           .polyline(prof).close()
           .extrude(-(Y_SEAT - PED_Y0)))
    body = body.union(ped)
    # round column standing on the shelf in front of the pedestal
    col = (cq.Workplane("XY", origin=(0, 0, LOW_Z))
           .center(xo - sx * COL_X, COL_Y).circle(COL_R)
           .extrude(SB_Z0 + 0.01 - LOW_Z))
    body = body.union(col)
    post_holes.append((xo - sx * POST_HX_LOW, -ZI + POST_HZ_LOW))

# ---------------- centre post on the front wall ----------------
body = body.union(box(-CP_W / 2, CP_W / 2, TF - 0.01, TF + CP_D, SB_Z0, SB_Z1))

# ---------------- snap catch under the ceiling ----------------
def catch_seg(x0, x1, yf):
    return (cq.Workplane("YZ", origin=(x0, 0, 0))
            .moveTo(yf, ZI + 0.01)
            .lineTo(Y_SEAT, ZI + 0.01)
            .lineTo(Y_SEAT, ZI - CATCH_H)
            .lineTo(Y_SEAT - 1.2, ZI - CATCH_H)
            .threePointArc((yf + 0.45 * (Y_SEAT - 1.2 - yf), ZI - 0.72 * CATCH_H),
                           (yf, ZI + 0.01))
            .close()
            .extrude(x1 - x0))

body = body.union(catch_seg(CATCH_X0, CATCH_XS, CATCH_Y0))
body = body.union(catch_seg(CATCH_XS - 0.01, CATCH_X1, CATCH_Y0B))

# ---------------- window with notch ----------------
xl, xr = -WIN_W / 2, WIN_W / 2
zt, zb = WIN_H / 2, -WIN_H / 2
win_pts = [
    (xl, zb), (xr, zb), (xr, -NOTCH_IN), (NOTCH_X, -NOTCH_OUT),
    (NOTCH_X, NOTCH_OUT), (xr, NOTCH_IN), (xr, zt), (xl, zt),
]
win = (cq.Workplane("XZ", origin=(0, -1.0, WIN_ZC))
       .polyline(win_pts).close()
       .extrude(-(TF + 2.0)))
body = body.cut(win)

# mounting holes
holes = (cq.Workplane("XZ", origin=(0, -1.0, WIN_ZC))
         .pushPoints([(sx * HOLE_DX, sz * HOLE_DZ) for sx in (-1, 1) for sz in (-1, 1)])
         .circle(HOLE_D / 2)
         .extrude(-(TF + 2.0)))
body = body.cut(holes)

# label pocket
pocket = (cq.Workplane("XZ", origin=(0, -1.0, POCK_ZC))
          .rect(POCK_W, POCK_H)
          .extrude(-(POCK_DEPTH + 1.0)))
body = body.cut(pocket)

# blind screw pilot holes for the back cover
for (hx, hz) in post_holes:
    body = body.cut(cq.Workplane("XZ", origin=(0, D + 1.0, 0))
                    .center(hx, hz).circle(POST_HOLE_D / 2)
                    .extrude(COVER_T + 1.0 + POST_HOLE_DEPTH))

result = body
